import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L_TIP = 100.0        # blade tip radius (from hub axis)
R_HUB = 26.0         # hub outer radius
HUB_LEN = 98.0       # hub length along Y (front face at Y=0)
BLADE_ROOT_LEN = 73.0  # blade chord at the hub (Y extent of blade root)
BLADE_TIP_LEN = 36.0   # blade chord at the tip
# blade thickness: sharp-ish leading edge (Y=0), thickening toward the back (Y=root len)
T_FRONT_HUB = 4.4    # at hub surface, leading edge
T_FRONT_TIP = 1.5    # at tip, leading edge
T_BACK_HUB = 5.8     # at hub surface, Y = BLADE_ROOT_LEN
T_BACK_TIP = 5.15    # at tip radius, Y = BLADE_ROOT_LEN (extrapolated, trimmed by slant)
ROOT_FILLET = 12.5   # blade-to-hub fillet radius
N_BLADES = 3
BLADE_START_ANGLE = 90.0   # first blade points straight up (+Z)
# blade directions in the XZ plane (degrees from +X toward +Z): 90, 210, 330
BLADE_ANGLES = [BLADE_START_ANGLE + i * 360.0 / N_BLADES for i in range(N_BLADES)]

# threaded front bore / through hole / rear counterbore
THREAD_R_MAJOR = 18.1
THREAD_R_MINOR = 16.7
THREAD_PITCH = 2.6
THREAD_DEPTH = 15.6   # threaded length
BORE_FLOOR_Y = 17.5   # flat floor of the threaded bore
THRU_R = 7.8
THRU_CBORE_R = 10.9     # shallow counterbore at the threaded-bore floor
THRU_CBORE_D = 1.5
THRU_CHAMFER_R = 1.0    # chamfer at the rear-bore floor
REAR_BORE_R = 25.2
REAR_BORE_DEPTH = 14.0

# side lug (pin boss with a small axial hole), midway between two blades
LUG_ANGLE = 30.0
LUG_DIST = 32.4
LUG_R = 4.4
LUG_HOLE_R = 2.4
LUG_Y0 = 30.5
LUG_Y1 = 41.5
LUG_FILLET = 3.0
LUG_EDGE_FILLET = 0.8


def xz_wp(y0=0.0):
    """Workplane parallel to XZ located at Y=y0 (local x=X, local y=Z)."""
    return cq.Workplane("XZ", origin=(0, y0, 0))


# ---------------- blade core ----------------
# blade half thickness: linear in radial coord u at the front and back sections,
# ruled (bilinear) in between
def half_t(u, y):
    k = (u - R_HUB) / (L_TIP - R_HUB)
    t0 = T_FRONT_HUB + (T_FRONT_TIP - T_FRONT_HUB) * k
    t1 = T_BACK_HUB + (T_BACK_TIP - T_BACK_HUB) * k
    return 0.5 * (t0 + (t1 - t0) * y / BLADE_ROOT_LEN)


def blade_prism(angle_deg, length):
    a = math.radians(angle_deg)
    ux, uz = math.cos(a), math.sin(a)
    nx, nz = -math.sin(a), math.cos(a)

    def section(y):
        pts = []
        for (u, sgn) in [(0.0, -1), (L_TIP, -1), (L_TIP, 1), (0.0, 1)]:
            h = half_t(u, y) * sgn
            pts.append((u * ux + h * nx, u * uz + h * nz))
        return pts

    return (xz_wp(0).polyline(section(0.0)).close()
            .workplane(offset=-length).polyline(section(length)).close()
            .loft(ruled=True))


# (cylinders rotated about Y so their seam lies at the underside, -Z)
core = (xz_wp(0).circle(R_HUB).extrude(-HUB_LEN)
        .rotate((0, 0, 0), (0, 1, 0), 90))
for ang in BLADE_ANGLES:
    core = core.union(blade_prism(ang, BLADE_ROOT_LEN))


# fillet the concave blade/hub junction edges (blade-plane / hub-cylinder
# intersection curves running the full root length at r ~ R_HUB)
def _root_edge(e):
    pts = [e.startPoint(), e.endPoint(), e.positionAt(0.5)]
    for p in pts:
        if abs(math.hypot(p.x, p.z) - R_HUB) > 0.05:
            return False
    ys = sorted([pts[0].y, pts[1].y])
    return ys[0] < 0.5 and ys[1] > BLADE_ROOT_LEN - 0.5


root_edges = [e for e in core.edges().vals() if _root_edge(e)]
core = core.newObject(root_edges).fillet(ROOT_FILLET)

# slanted trailing edge: cut each blade above the line (tip_len, L) -> (root_len, R)
for ang in BLADE_ANGLES:
    a = math.radians(ang)
    big = 40.0
    # cutter in the blade's local (Y, u) plane, extruded along blade normal
    ys = [BLADE_TIP_LEN, BLADE_ROOT_LEN, BLADE_ROOT_LEN, BLADE_TIP_LEN]
    us = [L_TIP, R_HUB, L_TIP + 10, L_TIP + 10]
    # build in a plane spanned by Y (local x) and u (local y), normal = blade normal
    ux, uz = math.cos(a), math.sin(a)
    nx, nz = -math.sin(a), math.cos(a)
    pl = cq.Plane(origin=(-nx * big / 2, 0, -nz * big / 2),
                  xDir=(0, 1, 0), normal=(nx, 0, nz))
    # check local y direction equals +u
    ydir = pl.yDir
    sign = 1.0 if (ydir.x * ux + ydir.z * uz) > 0 else -1.0
    pts = [(y, sign * u) for y, u in zip(ys, us)]
    cutter = cq.Workplane(pl).polyline(pts).close().extrude(big)
    core = core.cut(cutter)

body = core

# ---------------- side lug ----------------
la = math.radians(LUG_ANGLE)
lcx, lcz = LUG_DIST * math.cos(la), LUG_DIST * math.sin(la)
lug = (xz_wp(LUG_Y0).center(lcx, lcz).circle(LUG_R).extrude(-(LUG_Y1 - LUG_Y0)))
# web connecting lug to hub
web_len = LUG_DIST
web = (xz_wp(LUG_Y0)
       .transformed(rotate=(0, 0, LUG_ANGLE))
       .center(web_len / 2, 0)
       .rect(web_len, 2 * LUG_R)
       .extrude(-(LUG_Y1 - LUG_Y0)))
lug = lug.union(web)
body = body.union(lug)


def _lug_edge(e):
    # intersection curves of the lug web with the hub cylinder
    pts = [e.startPoint(), e.endPoint(), e.positionAt(0.5)]
    for p in pts:
        if abs(math.hypot(p.x, p.z) - R_HUB) > 0.05:
            return False
        if p.y < LUG_Y0 - 0.1 or p.y > LUG_Y1 + 0.1:
            return False
        ang = math.degrees(math.atan2(p.z, p.x))
        if abs(ang - LUG_ANGLE) > 25:
            return False
    return True


lug_edges = [e for e in body.edges().vals() if _lug_edge(e)]
body = body.newObject(lug_edges).fillet(LUG_FILLET)



# soften the outer edges of the lug's front and back faces
def _lug_face_edge(e):
    pts = [e.startPoint(), e.endPoint(), e.positionAt(0.5)]
    for p in pts:
        if not (abs(p.y - LUG_Y0) < 1e-3 or abs(p.y - LUG_Y1) < 1e-3):
            return False
        if math.hypot(p.x, p.z) < R_HUB + 0.3:
            return False
        ang = math.degrees(math.atan2(p.z, p.x))
        if abs(ang - LUG_ANGLE) > 25:
            return False
    return True


fe = [e for e in body.edges().vals() if _lug_face_edge(e)]
try:
    body = body.newObject(fe).fillet(LUG_EDGE_FILLET)
except Exception:
    pass  # small cosmetic round; keep the sharp lug edges if OCC cannot build it

# ---------------- bores ----------------
# one revolved cavity: threaded front bore (thread modelled as plain annular
# ridges), counterbored through hole, thin-walled rear counterbore
B_Y = HUB_LEN - REAR_BORE_DEPTH
prof = [(0.0, -1.0), (THREAD_R_MAJOR, -1.0), (THREAD_R_MAJOR, 0.0)]
n_th = int(round(THREAD_DEPTH / THREAD_PITCH))
for i in range(n_th):
    y0 = i * THREAD_PITCH
    prof.append((THREAD_R_MINOR, y0 + THREAD_PITCH * 0.5))
    if i < n_th - 1:
        prof.append((THREAD_R_MAJOR, y0 + THREAD_PITCH))
prof += [
    (THREAD_R_MINOR, BORE_FLOOR_Y),
    (THRU_CBORE_R, BORE_FLOOR_Y),
    (THRU_CBORE_R, BORE_FLOOR_Y + THRU_CBORE_D),
    (THRU_R, BORE_FLOOR_Y + THRU_CBORE_D),
    (THRU_R, B_Y - THRU_CHAMFER_R),
    (THRU_R + THRU_CHAMFER_R, B_Y),
    (REAR_BORE_R, B_Y),
    (REAR_BORE_R, HUB_LEN + 1.0),
    (0.0, HUB_LEN + 1.0),
]
cavity = (cq.Workplane("XY").polyline(prof).close()
          .revolve(360, (0, 0, 0), (0, 1, 0))
          .rotate((0, 0, 0), (0, 1, 0), 90))
body = body.cut(cavity)

# lug hole
lug_hole = xz_wp(LUG_Y0 - 1).center(lcx, lcz).circle(LUG_HOLE_R).extrude(-(LUG_Y1 - LUG_Y0 + 2))
body = body.cut(lug_hole)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
